import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 45.8            # overall height (bottom rim to top face)
R_BODY = 48.1       # skirt outer radius
WALL = 2.0          # skirt wall thickness

R_HOLE = 36.0       # opening in the top plate
STEP = 2.25         # radial growth of the bore from ring to ring (stepped funnel)

# stacked rings, depth measured from the top face: (top, bottom, outer radius)
TOP_PLATE = (0.0, 1.3, 47.35)
WIDE_RING = (2.55, 3.85, 50.0)
MID_RING = (4.95, 6.35, 48.8)
NECK = (7.15, 8.1, 47.55)       # lip on top of the skirt (ends in a 45 deg taper)
NECK_BORE_DEPTH = 8.35          # bottom of the inward flange on the skirt

R_IN = R_BODY - WALL


def z(d):
    """depth below the top face -> absolute height"""
    return H - d


def ring(top_d, bot_d, r_in, r_out):
    """plain annular ring between two depths"""
    return (
        cq.Workplane("XY")
        .workplane(offset=z(bot_d))
        .circle(r_out)
        .circle(r_in)
        .extrude(bot_d - top_d)
    )


# top plate with the central opening
plate = ring(TOP_PLATE[0], TOP_PLATE[1], R_HOLE, TOP_PLATE[2])
# two free thread rings below it, each with a slightly larger bore
wide = ring(WIDE_RING[0], WIDE_RING[1], R_HOLE + STEP, WIDE_RING[2])
mid = ring(MID_RING[0], MID_RING[1], R_HOLE + 2 * STEP, MID_RING[2])

# skirt: thin tube with a neck lip and an inward flange on top
r_flange = R_HOLE + 3 * STEP
skirt_pts = [
    (R_IN, 0.0),
    (R_BODY, 0.0),
    (R_BODY, z(NECK[1])),
    (NECK[2], z(NECK[1]) + (R_BODY - NECK[2])),
    (NECK[2], z(NECK[0])),
    (r_flange, z(NECK[0])),
    (r_flange, z(NECK_BORE_DEPTH)),
    (R_IN, z(NECK_BORE_DEPTH)),
]
skirt = (
    cq.Workplane("XZ")
    .polyline(skirt_pts)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

SEAM_ANGLE = 45.0   # park the periodic-surface seams on a silhouette line
solids = [
    w.val().rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_ANGLE)
    for w in (skirt, mid, wide, plate)
]
result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])

VIEW = {"azimuth": 45, "elevation": 26}
